import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L_TOTAL = 200.0        # overall length along X (block to block)
L_BLOCK = 11.2         # length of each end block along X
W_BLOCK = 48.6         # width of end blocks along Y
H_BLOCK = 5.7          # height of end blocks (below plate)

W_PLATE = 45.7         # width of the tray plate along Y
T_PLATE = 2.25         # plate thickness
LIP_W = 1.7            # side lip width
LIP_H = 1.7            # side lip height above plate top

PIN_D = 0.8            # thin centre pin
PIN_H = 17.7           # pin height above plate top

SPRING_Y = 19.3        # spring centre offset from mid-plane (each side)
SPRING_W = 1.3         # spring width along Y
SPRING_T = 1.75        # spring thickness
# spring centre line: horizontal at its free (left) end, bent with radius
# SPRING_R up to the slope SPRING_SLOPE, then straight up through the plate
SPRING_X0 = -81.5      # free end X
SPRING_Z0 = -6.45      # free end centre Z (plate underside is Z = 0)
SPRING_R = 360.0       # bend radius
SPRING_SLOPE = 0.17    # slope of the straight part
SPRING_X_END = 23.4    # upper end X (vertical end face)

OVERLAP = 0.1          # block tucked under plate end so the solids fuse

L_PLATE = L_TOTAL - 2 * L_BLOCK

# ---------------- plate with side lips (U-channel profile along X) ----------
hw = W_PLATE / 2
channel_pts = [
    (-hw, 0.0),
    (hw, 0.0),
    (hw, T_PLATE + LIP_H),
    (hw - LIP_W, T_PLATE + LIP_H),
    (hw - LIP_W, T_PLATE),
    (-hw + LIP_W, T_PLATE),
    (-hw + LIP_W, T_PLATE + LIP_H),
    (-hw, T_PLATE + LIP_H),
]
plate = (
    cq.Workplane("YZ", origin=(-L_PLATE / 2, 0, 0))
    .polyline(channel_pts)
    .close()
    .extrude(L_PLATE)
)

# ---------------- end blocks ----------------
for s in (-1, 1):
    blk_len = L_BLOCK + OVERLAP
    xc = s * (L_TOTAL / 2 - blk_len / 2)
    blk = (
        cq.Workplane("XY")
        .box(blk_len, W_BLOCK, H_BLOCK, centered=(True, True, False))
        .translate((xc, 0, -H_BLOCK))
    )
    plate = plate.union(blk)

# ---------------- centre pin ----------------
pin = (
    cq.Workplane("XY")
    .workplane(offset=T_PLATE - 0.1)
    .circle(PIN_D / 2)
    .extrude(PIN_H + 0.1)
    .rotate((0, 0, 0), (0, 0, 1), 135)   # park the cylinder seam at the back
)
plate = plate.union(pin)


# ---------------- leaf springs ----------------
def spring_solid(y0):
    th = math.atan(SPRING_SLOPE)
    h = SPRING_T / 2
    cx, cz = SPRING_X0, SPRING_Z0 + SPRING_R          # bend centre (above)

    def on_arc(rad, ang):
        return (cx + rad * math.sin(ang), cz - rad * math.cos(ang))

    ro, ri = SPRING_R + h, SPRING_R - h                # lower / upper faces
    lo_t = on_arc(ro, th)
    up_t = on_arc(ri, th)
    # straight run, cut off square to the plate (vertical end face at X_END)
    lo_e = (SPRING_X_END, lo_t[1] + (SPRING_X_END - lo_t[0]) * SPRING_SLOPE)
    up_e = (SPRING_X_END, up_t[1] + (SPRING_X_END - up_t[0]) * SPRING_SLOPE)

    wp = (
        cq.Workplane("XZ", origin=(0, y0, 0))
        .moveTo(*on_arc(ro, 0.0))
        .threePointArc(on_arc(ro, th / 2), lo_t)
        .lineTo(*lo_e)
        .lineTo(*up_e)
        .lineTo(*up_t)
        .threePointArc(on_arc(ri, th / 2), on_arc(ri, 0.0))
        .close()
        .extrude(SPRING_W / 2, both=True)
    )
    return wp


for s in (-1, 1):
    plate = plate.union(spring_solid(s * SPRING_Y))

result = plate

VIEW = {"azimuth": 45, "elevation": 26}
